import cadquery as cq

# ---- driving dimensions (mm) ----
D = 40.0            # outer diameter
H = 37.8            # overall height
TOP_FILLET = 4.0    # fillet on the outer top edge
SLOT_W = 12.7       # width of the cross slot in the top (along Y)
SLOT_D = 10.4       # depth of the slot from the top
HOLE_D = 8.5        # through hole in the slot floor
WALL = 2.0          # side wall thickness of the bottom bore
BORE_DEPTH = 16.7   # depth of the bore from the bottom face
SEAM_ANGLE = 180.0  # cosmetic: where the cylinder seam lies

R = D / 2.0

# main cylindrical body with rounded top edge
body = cq.Workplane("XY").circle(R).extrude(H)
# turn the cylinder so its parametric seam sits at the back (-X side)
body = body.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
body = body.faces(">Z").edges().fillet(TOP_FILLET)

# straight slot across the top, running along X
slot = (
    cq.Workplane("XY")
    .box(D + 10, SLOT_W, SLOT_D + 1, centered=(True, True, False))
    .translate((0, 0, H - SLOT_D))
)
body = body.cut(slot)

# blind bore from the underside (thin-walled skirt)
bore = cq.Workplane("XY").circle(R - WALL).extrude(BORE_DEPTH)
body = body.cut(bore)

# central through hole from slot floor into the bore
hole = cq.Workplane("XY").circle(HOLE_D / 2.0).extrude(H + 2).translate((0, 0, -1))
body = body.cut(hole)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
